import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
# U-shaped clip: open at the front (-Y), bent at the back (+Y)
L = 50.0          # depth along Y
W = 37.65         # width along X
H = 20.05         # overall height of the U (without lettering)
T_TOP = 3.6       # top plate thickness
T_BOT = 3.8       # bottom plate thickness
TB = 3.65         # back wall thickness
R_OUT = 5.7       # outer bend radius (side view)
R_IN = 1.2        # inner bend radius
Z_SPLIT = 7.0     # upper (rounded) / lower (crisp base) bodies meet on the straight back wall

# edge treatment
R_TOP_PLAN = 5.0  # plan corner radius, front corners of the top plate
R_BOT_PLAN = 2.1  # plan corner radius, front corners of the bottom plate
R_TOP_EDGE = 2.4  # round along the outer contour of the top plate and bend
R_IN_EDGE = 1.0   # round along the inner contour of the U
R_BOT_EDGE = 0.35 # small round along the underside contour

# lettering (embossed on the top plate)
TEXT_LINES = ["Project", "Spidey", "Sense"]
TEXT_SIZE = 6.1
TEXT_PITCH = 9.9       # baseline to baseline
TEXT_BASE0 = 0.13      # baseline Y of the middle line
TEXT_H = 0.9           # emboss height
FONT = "DejaVu Sans"

YF = -L / 2       # front (open) end
YB = L / 2        # back (bend)


def near(a, b, e=0.02):
    return abs(a - b) < e


def edges_where(wp, pred):
    """Workplane holding the edges of wp's solid whose bounding box satisfies pred."""
    return wp.newObject([e for e in wp.val().Edges() if pred(e.BoundingBox())])


def flat_edge(b, y=None, z=None):
    ok = True
    if y is not None:
        ok = ok and near(b.ymin, y) and near(b.ymax, y)
    if z is not None:
        ok = ok and near(b.zmin, z) and near(b.zmax, z)
    return ok


# ---------------- U profile (side view) extruded across the width ----------------
u = (cq.Workplane("YZ", origin=(-W / 2, 0, 0))
     .polyline([(YF, 0), (YB, 0), (YB, H), (YF, H), (YF, H - T_TOP),
                (YB - TB, H - T_TOP), (YB - TB, T_BOT), (YF, T_BOT)])
     .close().extrude(W))
# outer bends
u = edges_where(u, lambda b: flat_edge(b, y=YB, z=H) or flat_edge(b, y=YB, z=0)).fillet(R_OUT)
# inner bends
u = edges_where(u, lambda b: flat_edge(b, y=YB - TB, z=H - T_TOP)
                or flat_edge(b, y=YB - TB, z=T_BOT)).fillet(R_IN)

BIG = 4 * (L + W + H)
upper = u.intersect(cq.Workplane("XY").box(BIG, BIG, BIG, centered=(True, True, False))
                    .translate((0, 0, Z_SPLIT)))
lower = u.intersect(cq.Workplane("XY").box(BIG, BIG, Z_SPLIT, centered=(True, True, False)))

# ---------------- upper body: soft rounded top plate, upper bend, back wall ----------------
upper = edges_where(upper, lambda b: flat_edge(b, y=YF) and near(b.zmax, H)
                    and near(b.zmin, H - T_TOP)).fillet(R_TOP_PLAN)
# outer contour: top face edges, continuing round the bend and down the back wall
seam = YB - R_OUT
upper = edges_where(upper, lambda b: flat_edge(b, z=H)
                    and not flat_edge(b, y=seam)).fillet(R_TOP_EDGE)
# inner contour: underside of the top plate, round the inner bend, down the back wall
seam_t = YB - TB - R_IN
upper = edges_where(upper, lambda b: flat_edge(b, z=H - T_TOP)
                    and not flat_edge(b, y=seam_t)).fillet(R_IN_EDGE)

# ---------------- lower body: base plate with crisp underside ----------------
lower = edges_where(lower, lambda b: flat_edge(b, y=YF)
                    and near(b.zmin, 0) and near(b.zmax, T_BOT)).fillet(R_BOT_PLAN)
lower = edges_where(lower, lambda b: flat_edge(b, z=T_BOT)
                    and not flat_edge(b, y=seam_t)).fillet(R_IN_EDGE)
# small round along the underside contour
lower = edges_where(lower, lambda b: flat_edge(b, z=0)
                    and not flat_edge(b, y=seam)).fillet(R_BOT_EDGE)
# back corners rounded in plan to continue the back wall's edge round downwards
plan = (cq.Workplane("XY").sketch()
        .rect(W, L).vertices(">Y").fillet(R_TOP_EDGE).finalize()
        .extrude(Z_SPLIT))
lower = lower.intersect(plan)

body = upper.union(lower)

# ---------------- embossed lettering ----------------
for i, line in enumerate(TEXT_LINES):
    yb = TEXT_BASE0 + (1 - i) * TEXT_PITCH
    txt = (cq.Workplane("XY", origin=(0, yb, H - 0.05))
           .text(line, TEXT_SIZE, TEXT_H + 0.05, font=FONT,
                 halign="center", valign="bottom"))
    body = body.union(txt)

result = body
